import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 20.0            # depth of the part along Y
TAB_T = 4.0         # thickness of the upper hanging tab (X)
TAB_TOP = 86.5      # top of the tab (Z)
COL_TOP = 70.3      # top face of the column (Z)
COL_TR_X = 36.35    # X of column top-right corner
CORNER_X = 40.4     # X of inner corner / outer bottom corner
ARM_H = 20.0        # arm height (Z)
ARM_END = 118.35    # X of arm end face
SLANT_Z = 66.75     # Z where the slanted outer face meets the tab
LIP_D = 2.0         # lip depth below arm bottom at the end
CAP_X0 = 116.45     # X of cap inner face at Z = 0
CAP_SLOPE = 0.258   # dX/dZ tilt of cap inner face

# hook rib on the tab
RIB_BOT = 76.7
RIB_FLOOR = 80.45
RIB_LIP_TOP = 81.45
RIB_OUT = 8.05
RIB_LIP_IN = 6.05
R_RIB = 1.5         # rounded underside corner of the hook rib

# through holes in the column: (x, z, radius)
HOLES = [(21.35, 62.65, 5.05), (26.35, 47.65, 7.1), (29.85, 33.65, 4.15)]

R_BOT = 7.75        # height of the rounded (half-elliptic) arm underside
R_END = 3.0         # round over at the top of the arm end
R_COL = 1.0         # column top-right corner (profile)
R_SIDE = 2.0        # side edge rounds of the arm
R_COL_EDGE = 1.0    # side edge rounds of the column
R_HOLE = 1.0        # hole edge rounds
R_SLANT = 1.0       # slanted outer face edge rounds
R_TAB = 1.0         # tab edge rounds
R_LIP = 0.8         # lip bottom edge round


def cap_x(z):
    return CAP_X0 - CAP_SLOPE * z


def rounded_profile(wp, pts):
    """Closed polygon, pts = [(x, z, r)], r = corner radius (0 = sharp)."""
    n = len(pts)
    segs = []
    for i in range(n):
        px, pz, r = pts[i]
        if r <= 0:
            segs.append(("pt", (px, pz)))
            continue
        ax, az, _ = pts[i - 1]
        bx, bz, _ = pts[(i + 1) % n]
        u1 = (ax - px, az - pz)
        u2 = (bx - px, bz - pz)
        l1 = math.hypot(*u1)
        l2 = math.hypot(*u2)
        u1 = (u1[0] / l1, u1[1] / l1)
        u2 = (u2[0] / l2, u2[1] / l2)
        cosang = max(-1.0, min(1.0, u1[0] * u2[0] + u1[1] * u2[1]))
        th = math.acos(cosang) / 2.0
        d = r / math.tan(th)
        t1 = (px + u1[0] * d, pz + u1[1] * d)
        t2 = (px + u2[0] * d, pz + u2[1] * d)
        bv = (u1[0] + u2[0], u1[1] + u2[1])
        lb = math.hypot(*bv)
        bv = (bv[0] / lb, bv[1] / lb)
        cd = r / math.sin(th)
        c = (px + bv[0] * cd, pz + bv[1] * cd)
        m = (c[0] - bv[0] * r, c[1] - bv[1] * r)
        segs.append(("arc", t1, m, t2))
    # start point
    first = segs[0]
    start = first[1] if first[0] == "pt" else first[3]
    w = wp.moveTo(*start)
    order = segs[1:] + [segs[0]]
    for s in order:
        if s[0] == "pt":
            w = w.lineTo(*s[1])
        else:
            w = w.lineTo(*s[1]).threePointArc(s[2], s[3])
    return w.close()


# ---------------- side profile (XZ) ----------------
pts = [
    (0.0, SLANT_Z, 0.0),
    (CORNER_X, 0.0, 0.0),
    (CAP_X0, 0.0, 0.0),
    (cap_x(-LIP_D), -LIP_D, 0.0),
    (ARM_END, -LIP_D, 0.0),
    (ARM_END, ARM_H, R_END),
    (CORNER_X, ARM_H, 0.0),
    (COL_TR_X, COL_TOP, R_COL),
    (TAB_T, COL_TOP, 0.0),
    (TAB_T, RIB_BOT, 0.0),
    (RIB_OUT, RIB_BOT, R_RIB),
    (RIB_OUT, RIB_LIP_TOP, 0.4),
    (RIB_LIP_IN, RIB_LIP_TOP, 0.3),
    (RIB_LIP_IN, RIB_FLOOR, 0.0),
    (TAB_T, RIB_FLOOR, 0.0),
    (TAB_T, TAB_TOP, 0.0),
    (0.0, TAB_TOP, 0.6),
]

body = rounded_profile(cq.Workplane("XZ"), pts).extrude(W / 2.0, both=True)


# ---------------- edge selection helpers ----------------
def on_side(bb):
    """edge lies in the front (Y=-W/2) or back (Y=+W/2) face plane"""
    h = W / 2.0
    return ((abs(bb.ymin + h) < 1e-3 and abs(bb.ymax + h) < 1e-3) or
            (abs(bb.ymin - h) < 1e-3 and abs(bb.ymax - h) < 1e-3))


def pick(wp, pred):
    edges = [e for e in wp.val().Edges() if pred(e, e.BoundingBox())]
    return wp.newObject(edges)


# ---------------- side edge rounds (front & back faces) ----------------
# arm top + end round-over + end face (one tangent chain)
body = pick(body, lambda e, bb: on_side(bb) and
            bb.zmin > ARM_H - 0.01 and bb.zmax < ARM_H + 0.01 and
            bb.xmin > CORNER_X - 0.01).fillet(R_SIDE)

# column right edge + top corner + top edge
body = pick(body, lambda e, bb: on_side(bb) and
            bb.zmin > ARM_H - 0.5 and bb.xmax < CORNER_X + 0.01 and
            bb.zmax < COL_TOP + 0.01 and bb.xmin > TAB_T - 0.01 and
            bb.xmax > TAB_T + 0.01 and bb.zmax > COL_TOP - 2.0).fillet(R_COL_EDGE)

# slanted outer face edges
body = pick(body, lambda e, bb: on_side(bb) and e.geomType() == "LINE" and
            bb.xmin < 0.01 and bb.xmax > 30.0).fillet(R_SLANT)

# hanging tab outer/top edges
body = pick(body, lambda e, bb: on_side(bb) and (
    (bb.xmax < TAB_T + 0.01 and bb.xmin < TAB_T - 0.01 and
     bb.zmin > RIB_FLOOR - 0.01) or
    (bb.xmax < 0.01 and bb.zmin > SLANT_Z - 0.5))).fillet(R_TAB)

# ---------------- through holes with rounded entries ----------------
for (hx, hz, hr) in HOLES:
    cyl = cq.Workplane("XZ").center(hx, hz).circle(hr).extrude(W, both=True)
    body = body.cut(cyl)
body = pick(body, lambda e, bb: on_side(bb) and e.geomType() == "CIRCLE" and
            (bb.xmax - bb.xmin) > 2.0 * min(h[2] for h in HOLES) - 0.1).fillet(R_HOLE)

# ---------------- rounded arm underside (three-centre arc, ~half ellipse) ----------------
R_SIDE_ARC = 5.0    # radius of the two side arcs of the underside


def under_profile_pts():
    """(y, z) points of the underside curve: side arc, centre arc, side arc."""
    a = W / 2.0
    b = R_BOT
    r1 = R_SIDE_ARC
    # centre arc radius so that all three arcs are tangent
    r2 = ((a - r1) ** 2 + b ** 2 - r1 ** 2) / (2.0 * (b - r1))
    c1 = (a - r1, b)           # right side arc centre
    c2 = (0.0, r2)             # centre arc centre
    dx, dz = c1[0] - c2[0], c1[1] - c2[1]
    L = math.hypot(dx, dz)
    t = (c2[0] + dx / L * r2, c2[1] + dz / L * r2)   # tangency point (right)
    # mid point of right side arc
    a1 = math.atan2(t[1] - c1[1], t[0] - c1[0])
    am = (a1 + 0.0) / 2.0
    m1 = (c1[0] + r1 * math.cos(am), c1[1] + r1 * math.sin(am))
    return (a, b), m1, t


def under_cutter():
    L = ARM_END + 40.0
    (ya, za), m1, t = under_profile_pts()
    e = 3.0
    wp = (cq.Workplane("YZ").workplane(offset=-20.0)
          .moveTo(ya + e, za)
          .lineTo(ya, za)
          .threePointArc((m1[0], m1[1]), (t[0], t[1]))
          .threePointArc((0.0, 0.0), (-t[0], t[1]))
          .threePointArc((-m1[0], m1[1]), (-ya, za))
          .lineTo(-ya - e, za)
          .lineTo(-ya - e, -e)
          .lineTo(ya + e, -e)
          .close())
    cut = wp.extrude(L)
    # stop the cutter at the tilted inner face of the end cap
    big = 200.0
    stopper = (cq.Workplane("XZ")
               .polyline([(cap_x(-10.0), -10.0), (cap_x(30.0), 30.0),
                          (ARM_END + big, 30.0), (ARM_END + big, -10.0)])
               .close().extrude(W, both=True))
    return cut.cut(stopper)


body = body.cut(under_cutter())

# small round on the outer bottom edge of the end lip
body = pick(body, lambda e, bb: bb.zmax < -LIP_D + 0.01 and
            bb.xmin > ARM_END - 0.3 and (bb.ymax - bb.ymin) > 5.0).fillet(R_LIP)

result = body
